import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Spring-loaded caster: wheel on a short axle, a bent-wire torsion-spring fork
# (closed wire loop with two double-turn coils) and a mushroom mounting stud.
# Wheel axis = Y, wheel centre at the origin, mount above, coils toward +X.
# ---------------------------------------------------------------------------

# wheel
WHEEL_R = 50.0
WHEEL_W = 33.0
WHEEL_FILLET = 2.5
BOSS_R = 20.0
BOSS_T = 3.5
AXLE_R = 5.0
AXLE_L = 3.6
# wire spool (end cap) on each axle end
SPOOL_R = 17.3
SPOOL_L = 11.9
SPOOL_FILLET = 2.2

# wire
WIRE_R = 3.7
WRAP_R = 17.65          # centre-line radius of the wrap around the spool
Y_OUT = 29.4            # plane of the outer coil turn / hub legs
Y_IN = 21.2             # plane of the inner coil turn / top U
COIL_X = 73.1
COIL_R = 17.3
TOP_Z = 81.1            # top bar / U height (tangent to coil top)
COIL_Z = TOP_Z - COIL_R
U_X = 13.6              # X of the U bight behind the stud
U_BEND_R = 6.0
CROSS_X = 14.4          # lower cross bar over the wheel
CROSS_Z = 57.7
CROSS_BEND_R = 8.0
TRANS_END = 262.0       # coil angle (deg) where the pitch step ends
TRANS_PTS = 8           # interpolation stations along the pitch step

# mounting stud
MOUNT_X = 40.2
CAP_R = 21.3
CAP_Z0, CAP_Z1 = 90.7, 96.1
CAP_FILLET = 3.4
CAP_EDGE_FILLET = 0.6
DISK_R = 19.9
DISK_Z0 = 87.2
NECK_R = 17.2
NECK_Z0 = 84.9
PLATE_HX = 13.6
PLATE_HY = 19.7
PLATE_Z0 = 77.1
BODY_R = 17.8
FLANGE_R = 17.2
FLANGE_Z0 = 74.1
HEX_R = 10.2            # circumradius of the hex nut
HEX_Z0 = 63.4


def V(x, y, z):
    return cq.Vector(x, y, z)


# ------------------------------------------------------------------ wheel ---
def y_cyl(r, y0, y1):
    return cq.Solid.makeCylinder(r, y1 - y0, V(0, y0, 0), V(0, 1, 0))


wheel = (
    cq.Workplane()
    .add(y_cyl(WHEEL_R, -WHEEL_W / 2.0, WHEEL_W / 2.0))
    .edges()
    .fillet(WHEEL_FILLET)
)

body = wheel
for s in (1, -1):
    def span(r, a, b):
        # cylinder along Y between |y| = a and |y| = b on side s
        return y_cyl(r, min(s * a, s * b), max(s * a, s * b))

    y0 = WHEEL_W / 2.0
    ys = y0 + BOSS_T + AXLE_L
    outer = ">Y" if s > 0 else "<Y"
    boss = cq.Workplane().add(span(BOSS_R, y0 - 0.5, y0 + BOSS_T)).faces(outer).edges().fillet(0.8)
    axle = cq.Workplane().add(span(AXLE_R, y0 + BOSS_T - 0.3, ys + 0.3))
    spool = (
        cq.Workplane()
        .add(span(SPOOL_R, ys, ys + SPOOL_L))
        .faces(outer)
        .edges()
        .fillet(SPOOL_FILLET)
    )
    body = body.union(boss).union(axle).union(spool)


# ------------------------------------------------------------ wire path ----
def tangent_from_point(px, pz, r, left=True):
    """Tangent point on circle (centre origin, radius r) of a line from P,
    passing the circle on its -X side (left=True)."""
    d = math.hypot(px, pz)
    base = math.atan2(-pz, -px)
    off = math.asin(r / d)
    ang = base - off if left else base + off
    dx, dz = math.cos(ang), math.sin(ang)
    # perpendicular from centre towards the line
    nx, nz = -dz, dx
    if nx > 0:
        nx, nz = -nx, -nz
    return (r * nx, r * nz), (dx, dz)


def half_path(sy):
    """Edge groups making up one half of the closed wire loop, from the middle
    of the lower cross bar to the middle of the U bight (sy=+1: +Y side,
    sy=-1: the mirror-image -Y side)."""
    yo = sy * Y_OUT
    yi = sy * Y_IN
    edges = []

    # lower cross bar -> bend -> leg down to the hub (left side)
    (t1x, t1z), (ldx, ldz) = tangent_from_point(CROSS_X, CROSS_Z, WRAP_R, left=True)
    a = V(CROSS_X, 0, CROSS_Z)
    b = V(CROSS_X, yo - sy * CROSS_BEND_R, CROSS_Z)
    edges.append(cq.Edge.makeLine(a, b))
    bend_end = V(CROSS_X + CROSS_BEND_R * ldx, yo, CROSS_Z + CROSS_BEND_R * ldz)
    bc = V(CROSS_X + CROSS_BEND_R * ldx, yo - sy * CROSS_BEND_R, CROSS_Z + CROSS_BEND_R * ldz)
    m = math.sqrt(0.5)
    bmid = bc + (b - bc) * m + (bend_end - bc) * m
    edges.append(cq.Edge.makeThreePointArc(b, bmid, bend_end))
    t1 = V(t1x, yo, t1z)
    edges.append(cq.Edge.makeLine(bend_end, t1))

    # wrap around the spool (CCW in XZ seen from -Y), then leg to the coil
    th1 = math.atan2(t1z, t1x)
    dxc, dzc = COIL_X, COIL_Z
    dist = math.hypot(dxc, dzc)
    phi_d = math.atan2(dzc, dxc)
    th2 = phi_d - math.acos((WRAP_R - COIL_R) / dist)
    while th2 < th1:
        th2 += 2 * math.pi
    thm = 0.5 * (th1 + th2)
    t2 = V(WRAP_R * math.cos(th2), yo, WRAP_R * math.sin(th2))
    edges.append(
        cq.Edge.makeThreePointArc(
            t1, V(WRAP_R * math.cos(thm), yo, WRAP_R * math.sin(thm)), t2
        )
    )
    t3 = V(COIL_X + COIL_R * math.cos(th2), yo, COIL_Z + COIL_R * math.sin(th2))
    edges.append(cq.Edge.makeLine(t2, t3))

    def cp(th, y):
        return V(COIL_X + COIL_R * math.cos(th), y, COIL_Z + COIL_R * math.sin(th))

    # outer coil turn up to the top
    c0 = th2 - 2 * math.pi
    c1 = math.pi / 2
    edges.append(cq.Edge.makeThreePointArc(cp(c0, yo), cp(0.5 * (c0 + c1), yo), cp(c1, yo)))
    # pitch step: the wire moves from the outer-turn plane to the inner-turn
    # plane between the coil top and TRANS_END (smooth S-shaped pitch so it
    # stays tangent to both planar turns and clears the top bar)
    groups = [edges]
    c2 = math.radians(TRANS_END)

    def ramp(u):
        # smooth pitch profile 0 -> 1 with zero slope at both ends
        return 0.5 - 0.5 * math.cos(math.pi * u)

    n = TRANS_PTS
    pts = [cp(c1 + (c2 - c1) * i / n, yo + (yi - yo) * ramp(i / n)) for i in range(n + 1)]
    tan0 = V(-math.sin(c1), 0, math.cos(c1))
    tan1 = V(-math.sin(c2), 0, math.cos(c2))
    groups.append([cq.Edge.makeSpline(pts, tangents=[tan0, tan1])])
    edges = []
    groups.append(edges)

    # inner coil turn back to the top
    c3 = math.pi / 2 + 2 * math.pi
    edges.append(cq.Edge.makeThreePointArc(cp(c2, yi), cp(0.5 * (c2 + c3), yi), cp(c3, yi)))

    # top bar toward the stud, U bend, U bight to the centre plane
    p0 = V(COIL_X, yi, TOP_Z)
    p1 = V(U_X + U_BEND_R, yi, TOP_Z)
    edges.append(cq.Edge.makeLine(p0, p1))
    uc = V(U_X + U_BEND_R, yi - sy * U_BEND_R, TOP_Z)
    p2 = V(U_X, yi - sy * U_BEND_R, TOP_Z)
    umid = uc + (p1 - uc) * m + (p2 - uc) * m
    edges.append(cq.Edge.makeThreePointArc(p1, umid, p2))
    p3 = V(U_X, 0, TOP_Z)
    edges.append(cq.Edge.makeLine(p2, p3))
    return groups


def sweep_tube(edges, r):
    path = cq.Wire.assembleEdges(edges)
    e0 = edges[0]
    start = e0.startPoint()
    tang = e0.tangentAt(0)
    prof = cq.Wire.makeCircle(r, start, tang)
    return cq.Solid.sweep(prof, [], path, True, False, None, "right")


# each half of the loop is one continuous tangent sweep; the halves meet in
# the XZ mid-plane
wire = None
for side in (1, -1):
    path_edges = [e for grp in half_path(side) for e in grp]
    tube = cq.Workplane().add(sweep_tube(path_edges, WIRE_R))
    wire = tube if wire is None else wire.union(tube)

# --------------------------------------------------------- mounting stud ---
def z_cyl(r, z0, z1):
    return cq.Solid.makeCylinder(r, z1 - z0, V(MOUNT_X, 0, z0), V(0, 0, 1))


cap = (
    cq.Workplane()
    .add(z_cyl(CAP_R, CAP_Z0, CAP_Z1))
    .faces(">Z")
    .edges()
    .fillet(CAP_FILLET)
    .faces("<Z")
    .edges()
    .fillet(CAP_EDGE_FILLET)
)
stud = (
    cap.union(cq.Workplane().add(z_cyl(DISK_R, DISK_Z0, CAP_Z0 + 0.01)))
    .union(cq.Workplane().add(z_cyl(NECK_R, NECK_Z0, DISK_Z0 + 0.01)))
    .union(
        cq.Workplane("XY", origin=(MOUNT_X, 0, PLATE_Z0))
        .rect(2 * PLATE_HX, 2 * PLATE_HY)
        .extrude(NECK_Z0 - PLATE_Z0)
    )
    .union(cq.Workplane().add(z_cyl(BODY_R, PLATE_Z0, NECK_Z0)))
    .union(cq.Workplane().add(z_cyl(FLANGE_R, FLANGE_Z0, PLATE_Z0 + 0.01)))
    .union(
        cq.Workplane("XY", origin=(MOUNT_X, 0, HEX_Z0))
        .polygon(6, 2 * HEX_R)
        .extrude(FLANGE_Z0 - HEX_Z0 + 0.01)
    )
)

result = body.union(wire).union(stud)
